import math
import cadquery as cq
from OCP.BRepFeat import BRepFeat_SplitShape

# ---------------------------------------------------------------
# Servo holder box + name plate + round servo horn (three bodies)
# ---------------------------------------------------------------

# ---------- box (servo cradle) ----------
BOX_L = 60.0          # X
BOX_W = 31.0          # Y
BOX_H = 24.0          # Z
WALL = 3.0            # outer wall thickness
FLOOR = 3.0           # floor level of the filler zone under the block
TAB_FLOOR = 2.0       # floor level of the mounting-tab slot
BODY_FLOOR = 1.0      # floor level of the servo body pocket

BODY_X0, BODY_X1 = 11.2, 48.2      # servo body pocket (X)
TAB_X0, TAB_X1 = 3.0, 57.0         # mounting-tab slot (X)
TAB_Y1 = 9.1                       # tab slot back face (Y from front)
LIP_Y0 = 2.3                       # inner lip of front wall
U_X0, U_X1 = 6.0, 54.0             # U opening in the front wall
SILL_Z = 7.0                       # bottom of the U opening

HOLE_D = 2.0
HOLE_XS = (22.9, 36.7)
HOLE_Y = 15.0
SLOT_W = 2.0                       # cable slot along the back wall

# ---------- plate ----------
PL_L = 64.0
PL_W = 38.0
PL_T = 3.0
PL_CX, PL_CY = -41.15, 18.05
TXT_SIZE = 26.5                    # font size of the lettering
TXT_GROW = 0.55                    # stroke thickening (bold look)
TXT_DEPTH = 1.9
TXT_FONT = "DejaVu Serif"
K_POS = (-52.65, 18.15)            # glyph centres
S_POS = (-26.65, 18.1)
DOT_POS = (-38.7, 10.25)
DOT_D = 4.7
UND_RIM = 1.5                      # underside pocket rim width
UND_DEPTH = 0.9                    # underside pocket depth (letters leave a thin skin)

# ---------- horn ----------
HN_CX, HN_CY = -63.6, -20.2
HN_D = 19.8
HN_T = 2.0
HN_CHAMF = 0.3                     # rim chamfer
HUB_D = 8.8
HUB_H = 2.5
HN_HOLE_R = 7.05
HN_HOLE_D = 1.8
HN_CSK_D = 2.5
SPL_MIN_D = 5.0
SPL_MAJ_D = 5.7
SPL_N = 20
SPL_DEPTH = 3.0
CTR_HOLE_D = 2.3
SEAM_ANG = 112.5                   # orientation of the revolved body's seam


def _blk(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def box_part():
    b = cq.Workplane("XY").box(BOX_L, BOX_W, BOX_H, centered=False)
    # main cavity down to the upper floor level (tab zone + left filler zone)
    b = b.cut(_blk(TAB_X0, BODY_X1, WALL, BOX_W - WALL, FLOOR, BOX_H + 1))
    # mounting tab slot across the front of the cavity
    b = b.cut(_blk(TAB_X0, TAB_X1, WALL, TAB_Y1, TAB_FLOOR, BOX_H + 1))
    # deeper pocket for the servo body
    b = b.cut(_blk(BODY_X0, BODY_X1, TAB_Y1, BOX_W - WALL, BODY_FLOOR, BOX_H + 1))
    # inner lip of the front wall above the sill
    b = b.cut(_blk(TAB_X0, TAB_X1, LIP_Y0, WALL + 0.01, SILL_Z, BOX_H + 1))
    # U opening through the front wall
    b = b.cut(_blk(U_X0, U_X1, -1, WALL, SILL_Z, BOX_H + 1))
    # floor holes
    for hx in HOLE_XS:
        b = b.cut(cq.Workplane("XY").circle(HOLE_D / 2).extrude(BODY_FLOOR + 2)
                  .translate((hx, HOLE_Y, -1)))
    # cable slot through the floor along the back wall
    b = b.cut(_blk(BODY_X0, BODY_X1, BOX_W - WALL - SLOT_W, BOX_W - WALL, -1, BODY_FLOOR + 0.5))
    # filler block at the back-left of the cavity (added as its own feature)
    b = b.union(_blk(TAB_X0, BODY_X0, TAB_Y1, BOX_W - WALL, FLOOR, BOX_H), clean=False)
    # the right end face is split where the back wall starts (seam of the original model)
    solid = b.val()
    rface = [f for f in solid.Faces() if f.geomType() == "PLANE"
             and abs(f.Center().x - BOX_L) < 1e-6 and f.normalAt().x > 0.99]
    if rface:
        seam = cq.Edge.makeLine(cq.Vector(BOX_L, BOX_W - WALL, 0), cq.Vector(BOX_L, BOX_W - WALL, BOX_H))
        sp = BRepFeat_SplitShape(solid.wrapped)
        sp.Add(seam.wrapped, rface[0].wrapped)
        sp.Build()
        if sp.IsDone():
            sols = cq.Shape.cast(sp.Shape()).Solids()
            if len(sols) == 1 and sols[0].isValid():
                b = cq.Workplane("XY").add(sols[0])
    return b


def glyph_cutter(ch, size, grow, height):
    """Engraving tool for one glyph, strokes thickened by `grow` mm."""
    comp = cq.Compound.makeText(ch, size, 0.0, font=TXT_FONT, kind="regular",
                                halign="center", valign="center")
    solids = []
    for f in comp.Faces():
        try:
            w = f.outerWire().offset2D(grow, "arc")[0]
            ff = cq.Face.makeFromWires(w).toSplines()
        except Exception:
            ff = f
        solids.append(cq.Solid.extrudeLinear(ff, cq.Vector(0, 0, height)))
    return cq.Compound.makeCompound(solids)


def plate_part():
    p = cq.Workplane("XY").box(PL_L, PL_W, PL_T).translate((PL_CX, PL_CY, PL_T / 2))
    z0 = PL_T - TXT_DEPTH
    # engraved lettering "K.S" on the top face
    for ch, (cx, cy) in (("K", K_POS), ("S", S_POS)):
        g = glyph_cutter(ch, TXT_SIZE, TXT_GROW, TXT_DEPTH + 1)
        bb = g.BoundingBox()
        g = g.translate(cq.Vector(cx - (bb.xmin + bb.xmax) / 2, cy - (bb.ymin + bb.ymax) / 2, z0))
        p = p.cut(cq.Workplane().add(g))
    dot = (cq.Workplane("XY").workplane(offset=z0).center(*DOT_POS)
           .circle(DOT_D / 2).extrude(TXT_DEPTH + 1))
    p = p.cut(dot)
    # shallow pocket on the underside
    pk = (cq.Workplane("XY").rect(PL_L - 2 * UND_RIM, PL_W - 2 * UND_RIM)
          .extrude(UND_DEPTH).translate((PL_CX, PL_CY, 0)))
    p = p.cut(pk)
    return p


def horn_part():
    # flange disc with a small chamfer round its top rim
    h = cq.Workplane("XY").circle(HN_D / 2).extrude(HN_T)
    h = h.faces(">Z").edges().chamfer(HN_CHAMF)
    hub = cq.Workplane("XY").workplane(offset=HN_T).circle(HUB_D / 2).extrude(HUB_H)
    h = h.union(hub)
    # turn the turned body so the cylinder seams sit at the back
    h = h.rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)
    top = HN_T + HUB_H
    # 4 countersunk screw holes
    pts = [(HN_HOLE_R * math.cos(math.radians(a)), HN_HOLE_R * math.sin(math.radians(a)))
           for a in (0, 90, 180, 270)]
    h = (h.faces("<Z").workplane(centerOption="CenterOfBoundBox").pushPoints(pts)
         .hole(HN_HOLE_D))
    # simple countersink cones
    for (x, y) in pts:
        cone = cq.Solid.makeCone(HN_HOLE_D / 2, HN_CSK_D / 2, (HN_CSK_D - HN_HOLE_D) / 2,
                                 cq.Vector(x, y, HN_T - (HN_CSK_D - HN_HOLE_D) / 2))
        h = h.cut(cq.Workplane().add(cone))
    # splined bore
    bore = cq.Workplane("XY").workplane(offset=top - SPL_DEPTH).circle(SPL_MIN_D / 2).extrude(SPL_DEPTH + 1)
    h = h.cut(bore)
    tooth_w = math.pi * SPL_MIN_D / SPL_N / 2
    for i in range(SPL_N):
        a = 360.0 * i / SPL_N
        t = (cq.Workplane("XY").workplane(offset=top - SPL_DEPTH)
             .center((SPL_MIN_D / 2 + SPL_MAJ_D / 2) / 2 - 0.1, 0)
             .rect((SPL_MAJ_D - SPL_MIN_D) / 2 + 0.2, tooth_w)
             .extrude(SPL_DEPTH + 1)
             .rotate((0, 0, 0), (0, 0, 1), a))
        h = h.cut(t)
    # through hole
    h = h.cut(cq.Workplane("XY").workplane(offset=-1).circle(CTR_HOLE_D / 2).extrude(top + 2))
    return h.translate((HN_CX, HN_CY, 0))


box = box_part()
plate = plate_part()
horn = horn_part()

# three separate bodies kept side by side (no merging between them)
result = box.union(plate, clean=False).union(horn, clean=False)

VIEW = {"azimuth": 45, "elevation": 26}
